"""Engraved key-ring tag "TecnoLab / La Rueca".

A flat rectangular plate with rounded corners standing in the XZ plane
(thickness along Y), a vertical key-ring slot near the -X end, and the same
two lines of lettering engraved into BOTH faces (each reading correctly from
its own side, kept in the region away from the slot).
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 80.0            # plate length (X)
H = 38.8            # plate height (Z)
T = 4.1             # plate thickness (Y)
CORNER_R = 3.0      # plate corner radius (edges parallel to Y)

SLOT_W = 5.2        # key-ring slot width (X)
SLOT_L = 12.5       # key-ring slot overall length (Z)
SLOT_CX = -W / 2 + 3.9   # slot centre X (centred in Z)

TXT_DEPTH = 1.3     # engraving depth on each face
EPS = 0.3           # cutting-tool overshoot beyond the face
CAP_H = 10.1        # capital height of the lettering
FONT = "DejaVu Sans"
FONT_KIND = "bold"
STROKE_TRIM = 0.08  # stroke thinning per side (target face is a touch lighter)

# lettering boxes on the front face: (text, left x, right x, baseline z)
LINES = [
    ("TecnoLab", -29.7, 36.7, 2.75),
    ("La Rueca", -28.45, 33.1, -12.95),
]

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- plate ----------------
plate = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(T / 2, both=True)
    .edges("|Y")
    .fillet(CORNER_R)
)

slot = (
    cq.Workplane("XZ")
    .center(SLOT_CX, 0)
    .slot2D(SLOT_L, SLOT_W, angle=90)
    .extrude(T, both=True)
)
plate = plate.cut(slot)


# ---------------- lettering ----------------
def thin_face(f, d):
    """Shrink a planar glyph face by d on every side (outline in, holes out)."""
    if d <= 0:
        return f
    try:
        outer = f.outerWire().offset2D(-d, "arc")[0]
        inner = [w.offset2D(d, "arc")[0] for w in f.innerWires()]
        g = cq.Face.makeFromWires(outer, inner)
        return g if g.isValid() and g.Area() > 0 else f
    except Exception:
        return f


def line_solid(txt, x0, x1, zb):
    """Engraving tool for one line of lettering, lying in XY (glyph up = +Y)
    and extruded +Z: glyph outlines thinned by STROKE_TRIM, fitted to the
    measured box [x0, x1] with the baseline at zb, then extruded."""
    fs = CAP_H / 0.729                      # cap height -> font size
    flat = cq.Compound.makeText(
        txt, fs, 0, font=FONT, kind=FONT_KIND, halign="left", valign="bottom"
    )
    flat = cq.Compound.makeCompound([thin_face(f, STROKE_TRIM) for f in flat.Faces()])
    bb = flat.BoundingBox()
    sx = (x1 - x0) / (bb.xmax - bb.xmin)
    # horizontal fit (the target face is narrower than the stand-in font);
    # the general transform also turns every curve into a plain B-spline
    m = cq.Matrix([[sx, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0]])
    flat = flat.transformGeometry(m)
    bb = flat.BoundingBox()
    tools = [
        cq.Solid.extrudeLinear(f, cq.Vector(0, 0, TXT_DEPTH + EPS))
        for f in flat.Faces()
    ]
    return cq.Compound.makeCompound(tools).translate(cq.Vector(x0 - bb.xmin, zb, 0))


def engraving(front=True):
    solids = []
    for txt, x0, x1, zb in LINES:
        s = line_solid(txt, x0, x1, zb)
        # map the XY lettering onto the front face: rotate +90 deg about X
        # (Y->Z, Z->-Y), then shift so the tool starts EPS outside y = -T/2
        # and reaches TXT_DEPTH into the plate
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), 90)
        s = s.translate(cq.Vector(0, -T / 2 + TXT_DEPTH, 0))
        if not front:
            # back face: same line box, turned 180 deg about its own vertical
            # centre line so it reads correctly from behind
            xc = 0.5 * (x0 + x1)
            s = s.rotate(cq.Vector(xc, 0, 0), cq.Vector(xc, 0, 1), 180)
        solids.append(s)
    return cq.Compound.makeCompound(solids)


result = plate.cut(engraving(True)).cut(engraving(False))
